import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# origin: axis of the top/bottom flange, Z=0 at body mid-height
R_CYL = 48.3          # radius of rounded front housing
CYL_YC = 1.5          # Y offset of housing axis
H_CYL = 64.0          # height of rounded housing
CH_CYL = 6.0          # chamfer on housing top/bottom rim
X_LEFT_CUT = -39.0    # flat cut on the -X side of the housing

CORE_W = 56.0         # core block width (X)
CORE_Y0 = -21.5       # core front face
CORE_Y1 = 70.5        # core back face
CORE_H = 66.0         # core height (top plate level)

PANEL_X = 38.5        # +X rear side panel face
PANEL_PAD = 1.3       # raised cover on the +X panel
PANEL_Y0 = 20.0
PANEL_Y1 = 66.0
PANEL_H = 64.0
JOIN_R = 3.0          # concave blend housing -> side panel

SLOT_W = 14.0         # slot in front top/bottom
SLOT_D = 6.0

FL_D = 38.5           # flange ring diameter
FL_H = 5.0            # flange ring height
FL_BORE = 17.5
FL_BORE_DEPTH = 5.0
FL_REC = 23.5
FL_BC = 31.5
FL_HOLE = 2.6

BAR_Y0 = 57.0         # frame bars (top / bottom)
BAR_Y1 = 80.0
BAR_T = 3.2
FRAME_Y0 = 76.8       # frame back wall (inner face)
FRAME_RI = 1.0        # inner bend radius of the sheet-metal frame
FRAME_H = CORE_H + 2 * BAR_T

PL_W = 51.6           # handle plate
PL_H = 94.0
PL_Y0 = 80.0
PL_T = 10.5
PL_R = 10.0
PL_BACK_R = 2.0       # rounding of the plate's rear edge

HD_R = 20.0           # handle grip radius
HD_TIP = 190.0        # handle tip Y
NECK_R0 = 46.0        # trumpet radius at the plate
NECK_FR = 26.0        # trumpet fillet radius
NECK_CLIP_Z = 37.8

HOLE_X = 15.8         # front counterbored holes
HOLE_Z = 12.0
HOLE_CB = 13.5
HOLE_D = 5.0

SCREW_X = 22.0
SCREW_Y_TOP = -15.0
SCREW_Y_BOT = -18.0

STUB_COLLAR_D = 15.7  # pivot stub under the bottom flange
STUB_COLLAR_H = 3.9
STUB_PIN_D = 8.7
STUB_PIN_H = 4.9

# ---------------- rounded housing ----------------
cyl = (
    cq.Workplane("XY")
    .circle(R_CYL)
    .extrude(H_CYL)
    .translate((0, CYL_YC, -H_CYL / 2))
    .edges("%CIRCLE")
    .chamfer(CH_CYL)
)
# clip -X side
clip = cq.Workplane("XY").box(200, 200, 200).translate((X_LEFT_CUT + 100, 0, 0))
cyl = cyl.intersect(clip)
# remove the part behind the front lip on the -X side
notch = (
    cq.Workplane("XY")
    .box(40, 120, 100)
    .translate((-CORE_W / 2 - 20, CORE_Y0 + 60, 0))
)
cyl = cyl.cut(notch)

# ---------------- core block (incl. top/bottom plates) ----------------
core = (
    cq.Workplane("XY")
    .box(CORE_W, CORE_Y1 - CORE_Y0, CORE_H)
    .translate((0, (CORE_Y0 + CORE_Y1) / 2, 0))
)

# ---------------- +X rear side panel ----------------
panel = (
    cq.Workplane("XY")
    .box(PANEL_X - CORE_W / 2 + 1, PANEL_Y1 - PANEL_Y0, PANEL_H)
    .translate(((PANEL_X + CORE_W / 2 - 1) / 2, (PANEL_Y0 + PANEL_Y1) / 2, 0))
    .edges("|Y and >X")
    .fillet(4.0)
)

body = core.union(cyl).union(panel)
# concave blend between round housing and the side panel
y_join = CYL_YC + math.sqrt(R_CYL ** 2 - PANEL_X ** 2)
try:
    body = body.edges(
        cq.selectors.BoxSelector((PANEL_X - 0.5, y_join - 1.5, -20), (PANEL_X + 0.5, y_join + 1.5, 20))
    ).fillet(JOIN_R)
except Exception:
    pass

# raised cover on the +X side panel
y_pad0 = y_join + JOIN_R + 0.8
pad = (
    cq.Workplane("XY")
    .box(PANEL_PAD + 0.5, PANEL_Y1 - y_pad0, 56)
    .edges("|Z and >X and <Y")
    .fillet(1.2)
    .translate((PANEL_X + (PANEL_PAD - 0.5) / 2, (y_pad0 + PANEL_Y1) / 2, 0))
)
body = body.union(pad)

# ---------------- shallow steps on the top plate ----------------
# middle region (between Y=16 and the notched seam) and rear region
notch_pts = [
    (-CORE_W / 2 - 1, 41.3), (-18.5, 41.3), (-18.5, 37.9), (-11.8, 30.7),
    (11.8, 30.7), (18.5, 37.9), (18.5, 41.3), (CORE_W / 2 + 1, 41.3),
    (CORE_W / 2 + 1, BAR_Y0 + 2), (-CORE_W / 2 - 1, BAR_Y0 + 2),
]
rear_step = (
    cq.Workplane("XY", origin=(0, 0, CORE_H / 2))
    .polyline(notch_pts).close()
    .extrude(0.6)
)
rear_step = rear_step.intersect(
    cq.Workplane("XY").box(CORE_W, 200, 200)
)
mid_step = (
    cq.Workplane("XY", origin=(0, 0, CORE_H / 2))
    .center(0, (16.0 + 45.0) / 2)
    .rect(CORE_W, 45.0 - 16.0)
    .extrude(0.3)
)
body = body.union(rear_step).union(mid_step)

# ---------------- front slots (top and bottom) ----------------
for sgn in (1, -1):
    slot = (
        cq.Workplane("XY")
        .box(SLOT_W, 40, 20)
        .translate((0, CORE_Y0 - 20, sgn * (H_CYL / 2 - SLOT_D + 10)))
    )
    body = body.cut(slot)

# ---------------- pockets in back face of the front-left lip ----------------
LIP_PK_D = 5.5
for z0, z1 in ((-25, -9.5), (-7.5, 7.5), (9.5, 25)):
    pk = (
        cq.Workplane("XY")
        .box(8.3, 2 * LIP_PK_D, z1 - z0)
        .translate((-33.15, CORE_Y0, (z0 + z1) / 2))
    )
    body = body.cut(pk)

# ---------------- front counterbored holes ----------------
for hx in (-HOLE_X, HOLE_X):
    for hz in (-HOLE_Z, HOLE_Z):
        cb = (
            cq.Workplane("XZ", origin=(hx, -31.0, hz))
            .circle(HOLE_CB / 2)
            .extrude(30)
        )
        th = (
            cq.Workplane("XZ", origin=(hx, -17.0, hz))
            .circle(HOLE_D / 2)
            .extrude(20)
        )
        body = body.cut(cb).cut(th)

# ---------------- flange rings ----------------
top_fl = (
    cq.Workplane("XY", origin=(0, 0, CORE_H / 2))
    .circle(FL_D / 2)
    .extrude(FL_H)
    .faces(">Z").edges()
    .chamfer(0.6)
)
bot_fl = (
    cq.Workplane("XY", origin=(0, 0, -CORE_H / 2))
    .circle(FL_D / 2)
    .extrude(-FL_H)
    .faces("<Z").edges()
    .chamfer(0.6)
)
body = body.union(top_fl).union(bot_fl)

z_fl_top = CORE_H / 2 + FL_H
# top: shallow recess + chamfered bore
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, z_fl_top - 0.8)).circle(FL_REC / 2).extrude(2)
)
bore = cq.Solid.makeCone(FL_BORE / 2, FL_BORE / 2 + 1.0, 1.0,
                         pnt=cq.Vector(0, 0, z_fl_top - 1.8), dir=cq.Vector(0, 0, 1))
body = body.cut(cq.Workplane("XY").add(bore))
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, z_fl_top - FL_BORE_DEPTH)).circle(FL_BORE / 2).extrude(FL_BORE_DEPTH - 1.0)
)
# bolt circle holes top & bottom (with small countersink)
for i in range(8):
    a = math.radians(45 * i)
    px, py = FL_BC / 2 * math.cos(a), FL_BC / 2 * math.sin(a)
    body = body.cut(
        cq.Workplane("XY", origin=(px, py, CORE_H / 2 - 3)).circle(FL_HOLE / 2).extrude(10)
    )
    body = body.cut(cq.Workplane("XY").add(
        cq.Solid.makeCone(FL_HOLE / 2, FL_HOLE / 2 + 0.8, 0.8,
                          pnt=cq.Vector(px, py, z_fl_top - 0.8), dir=cq.Vector(0, 0, 1))))
    body = body.cut(
        cq.Workplane("XY", origin=(px, py, -CORE_H / 2 + 3)).circle(FL_HOLE / 2).extrude(-10)
    )
    body = body.cut(cq.Workplane("XY").add(
        cq.Solid.makeCone(FL_HOLE / 2, FL_HOLE / 2 + 0.8, 0.8,
                          pnt=cq.Vector(px, py, -z_fl_top + 0.8), dir=cq.Vector(0, 0, -1))))

# bottom stub (washer + pin)
stub = (
    cq.Workplane("XY", origin=(0, 0, -CORE_H / 2 - FL_H))
    .circle(STUB_COLLAR_D / 2).extrude(-STUB_COLLAR_H)
    .faces("<Z").workplane()
    .circle(STUB_PIN_D / 2).extrude(STUB_PIN_H)
    .faces("<Z").edges()
    .chamfer(0.6)
)
body = body.union(stub)

# ---------------- frame: bent sheet-metal U (top bar, back wall, bottom bar) ----------------
zt_o = CORE_H / 2 + BAR_T      # outer face of the bars
zt_i = CORE_H / 2              # inner face of the bars
yw_i = FRAME_Y0                # inner face of the back wall
yw_o = PL_Y0                   # outer face of the back wall (against the plate)
ro = FRAME_RI + BAR_T
c45 = math.sqrt(0.5)
frame_prof = (
    cq.Workplane("YZ", origin=(-CORE_W / 2, 0, 0))
    .moveTo(BAR_Y0, zt_o)
    .lineTo(yw_o - ro, zt_o)
    .threePointArc((yw_o - ro + ro * c45, zt_o - ro + ro * c45), (yw_o, zt_o - ro))
    .lineTo(yw_o, -zt_o + ro)
    .threePointArc((yw_o - ro + ro * c45, -zt_o + ro - ro * c45), (yw_o - ro, -zt_o))
    .lineTo(BAR_Y0, -zt_o)
    .lineTo(BAR_Y0, -zt_i)
    .lineTo(yw_i - FRAME_RI, -zt_i)
    .threePointArc((yw_i - FRAME_RI + FRAME_RI * c45, -zt_i + FRAME_RI - FRAME_RI * c45),
                   (yw_i, -zt_i + FRAME_RI))
    .lineTo(yw_i, zt_i - FRAME_RI)
    .threePointArc((yw_i - FRAME_RI + FRAME_RI * c45, zt_i - FRAME_RI + FRAME_RI * c45),
                   (yw_i - FRAME_RI, zt_i))
    .lineTo(BAR_Y0, zt_i)
    .close()
)
frame = frame_prof.extrude(CORE_W)
try:
    frame = frame.edges(
        cq.selectors.BoxSelector((-CORE_W, BAR_Y0 - 0.5, -60), (CORE_W, BAR_Y0 + 0.5, 60))
    ).edges("|Z").fillet(3.0)
except Exception:
    pass
body = body.union(frame)

# ---------------- screws on top / bottom ----------------
for sgn in (1, -1):
    ztop = sgn * CORE_H / 2
    zbar = sgn * (CORE_H / 2 + BAR_T)
    d = 1 if sgn > 0 else -1
    sy = SCREW_Y_TOP if sgn > 0 else SCREW_Y_BOT
    for sx in (-SCREW_X, SCREW_X):
        # front counterbored screws in top / bottom plate
        body = body.cut(
            cq.Workplane("XY", origin=(sx, sy, ztop - d * 2.0)).circle(3.8).extrude(d * 5)
        )
        body = body.cut(
            cq.Workplane("XY", origin=(sx, sy, ztop - d * 8)).circle(1.7).extrude(d * 8)
        )
        # countersunk screws in the frame bar
        csk = cq.Solid.makeCone(1.7, 3.8, 2.1, pnt=cq.Vector(sx, 63.5, zbar - d * 2.1),
                                dir=cq.Vector(0, 0, d))
        body = body.cut(cq.Workplane("XY").add(csk))
        body = body.cut(
            cq.Workplane("XY", origin=(sx, 63.5, zbar - d * 8)).circle(1.7).extrude(d * 8)
        )

# small blind hole in the bottom plate
body = body.cut(
    cq.Workplane("XY", origin=(24.0, 13.0, -CORE_H / 2 - 1)).circle(1.3).extrude(6)
)

# ---------------- -X side: stepped rectangular window and small holes ----------------
WIN_Y = 30.5
body = body.cut(
    cq.Workplane("XY").box(1.6, 23, 12.6).translate((-CORE_W / 2, WIN_Y, 24.3))
)
body = body.cut(
    cq.Workplane("XY").box(12, 19, 7.4).translate((-CORE_W / 2, WIN_Y + 0.8, 24.6))
)
for (yy, zz) in ((55.0, 12), (55.0, -13), (8, 12), (8, -13)):
    body = body.cut(
        cq.Workplane("YZ", origin=(-CORE_W / 2 - 2, yy, zz)).circle(1.2).extrude(7)
    )

# ---------------- handle plate ----------------
plate = (
    cq.Workplane("XY")
    .box(PL_W, PL_T, PL_H)
    .edges("|Y")
    .fillet(PL_R)
    .faces(">Y")
    .edges()
    .fillet(PL_BACK_R)
    .translate((0, PL_Y0 + PL_T / 2, 0))
)

# ---------------- handle (trumpet neck + grip + dome, one smooth face) ----------------
y_pb = PL_Y0 + PL_T          # plate back face
y_dome = HD_TIP - HD_R
# profile drawn in the YZ plane (local x = world Y, local y = world Z), radius toward -Z
# single tangent-constrained spline: concave fillet -> straight grip -> round dome
s45 = math.sqrt(0.5)
yc_f = y_pb + NECK_FR
pts = []
tgs = []
# concave neck fillet (quarter arc, centre (yc_f, -NECK_R0))
for a in (0.0, 22.5, 45.0, 67.5, 90.0):
    t = math.radians(a)
    pts.append((yc_f - NECK_FR * math.cos(t), -NECK_R0 + NECK_FR * math.sin(t)))
    tgs.append((math.sin(t), math.cos(t)))
# straight grip
for yy in (yc_f + (y_dome - yc_f) / 3.0, yc_f + 2.0 * (y_dome - yc_f) / 3.0, y_dome):
    pts.append((yy, -HD_R))
    tgs.append((1.0, 0.0))
# round dome (quarter arc, centre (y_dome, 0)), ends just short of the axis
for a in (22.5, 45.0, 67.5, 89.4):
    t = math.radians(a)
    pts.append((y_dome + HD_R * math.sin(t), -HD_R * math.cos(t)))
    tgs.append((math.cos(t), math.sin(t)))
prof = (
    cq.Workplane("YZ")
    .moveTo(y_pb - 4, 0)
    .lineTo(y_pb - 4, -NECK_R0)
    .lineTo(pts[0][0], pts[0][1])
    .spline(pts[1:], tangents=tgs, includeCurrent=True, scale=False)
    .lineTo(pts[-1][0], 0.0)
    .close()
)
handle = prof.revolve(360, (0, 0, 0), (1, 0, 0))
hclip = (
    cq.Workplane("XY")
    .box(PL_W, 200, 2 * NECK_CLIP_Z)
    .translate((0, y_pb - 4 + 100, 0))
)
handle = handle.intersect(hclip)
# small screw holes in the neck
for hx in (-11.8, 11.8):
    for sgn in (1, -1):
        handle = handle.cut(
            cq.Workplane("XY", origin=(hx, y_pb + 7.9, sgn * 15.0))
            .circle(1.5).extrude(sgn * 20)
        )

result = body.union(plate).union(handle)
